import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
T_PLATE = 3.6            # plate / frame thickness
PLATE_W = 59.6           # central plate width  (X)
PLATE_L = 83.36          # central plate length (Y)
PLATE_R = 4.2            # central plate corner radius (front)
PLATE_R_BACK = 3.0       # central plate corner radius (back)

# mounting holes (rectangular pattern)
HOLE_X = 54.6
HOLE_Y = 36.9
HOLE_D = 3.2
HOLE_CH = 0.35

# posts / tabs
POST_R = 3.0
TAB_R = 4.65             # half width of the oblong tab
TAB_C = 4.8              # distance between the two tab end centres
TAB_T = 3.85
TAB_TOP = 15.63
TAB_BOT = TAB_TOP - TAB_T
POST_OFF = TAB_C + TAB_R - POST_R   # hole centre -> post centre (post flush w/ tab end)

# back posts: tab points outward in X ; front posts: tab points forward in -Y
BACK_POST = (HOLE_X - POST_OFF, HOLE_Y)
FRONT_POST = (HOLE_X, -HOLE_Y + POST_OFF)

# hourglass frame
WAIST = (28.66, -1.12)   # sharp waist corner (right side) before rounding
WAIST_FILLET = 9.0
ARM_W = 6.2              # width of the diagonal arms
TRI_R = 1.0              # corner radius of triangular windows

# curved ribs on the rails
WALL_T_FRONT = 2.8
WALL_T_BACK = 2.3
WALL_R_FRONT = 215.0
WALL_R_BACK = 197.0
WALL_DIP_FRONT = 0.05    # arc lowest point below the plate top
WALL_DIP_BACK = -0.03    # back rib stays (just) continuous
CB_D = 6.8               # counterbore under each tab hole
CB_DEPTH = 1.5
TAB_EDGE_R = 0.4
RIB_POST_FILLET = 1.5


def mx(p):
    return (-p[0], p[1])


def tangent_point(w, c, r, side):
    """Tangent point on circle (c, r) of a line from external point w.
    side=+1 / -1 selects which of the two tangents."""
    dx, dy = c[0] - w[0], c[1] - w[1]
    d = math.hypot(dx, dy)
    a = math.asin(r / d) * side
    L = math.sqrt(d * d - r * r)
    ux, uy = dx / d, dy / d
    vx = ux * math.cos(a) - uy * math.sin(a)
    vy = ux * math.sin(a) + uy * math.cos(a)
    return (w[0] + L * vx, w[1] + L * vy), (vx, vy)


# ---------------- frame outline (left side computed, mirrored) ----------------
B = mx(BACK_POST)
F = mx(FRONT_POST)
W = mx(WAIST)
# outer tangents (away from part centre -> toward -X)
tB, dB = tangent_point(W, B, POST_R, -1)
tF, dF = tangent_point(W, F, POST_R, +1)
if tB[0] > B[0]:
    tB, dB = tangent_point(W, B, POST_R, +1)
if tF[0] > F[0]:
    tF, dF = tangent_point(W, F, POST_R, -1)

bTop = (B[0], B[1] + POST_R)
fBot = (F[0], F[1] - POST_R)
outline = [bTop, tB, W, tF, fBot, mx(fBot), mx(tF), mx(W), mx(tB), mx(bTop)]

frame = cq.Workplane("XY").polyline(outline).close().extrude(T_PLATE)
frame = frame.edges("|Z").edges(cq.selectors.BoxSelector(
    (W[0] - 0.5, W[1] - 0.5, -1), (W[0] + 0.5, W[1] + 0.5, T_PLATE + 1))).fillet(WAIST_FILLET)
frame = frame.edges("|Z").edges(cq.selectors.BoxSelector(
    (-W[0] - 0.5, W[1] - 0.5, -1), (-W[0] + 0.5, W[1] + 0.5, T_PLATE + 1))).fillet(WAIST_FILLET)
for p in (B, F, mx(B), mx(F)):
    frame = frame.union(cq.Workplane("XY").center(*p).circle(POST_R)
                        .extrude(T_PLATE))
plate = (cq.Workplane("XY").rect(PLATE_W, PLATE_L).extrude(T_PLATE)
         .edges("|Z").edges("<Y").fillet(PLATE_R)
         .edges("|Z").edges(">Y").fillet(PLATE_R_BACK))
base = frame.union(plate)


def fillet_vertical(shape, pts, r, tol=0.6):
    sel = []
    for e in shape.Edges():
        a = e.startPoint()
        b = e.endPoint()
        if abs(a.x - b.x) > 1e-6 or abs(a.y - b.y) > 1e-6:
            continue
        for p in pts:
            if math.hypot(a.x - p[0], a.y - p[1]) < tol:
                sel.append(e)
                break
    if not sel:
        return shape
    return shape.fillet(r, sel)


solid = base.val()
# concave junctions plate / rails
xj = PLATE_W / 2 - PLATE_R_BACK
yj = PLATE_L / 2 - PLATE_R_BACK
yb = bTop[1]
xb = xj + math.sqrt(max(PLATE_R_BACK ** 2 - (yb - yj) ** 2, 0.0))
solid = fillet_vertical(solid, [(xb, yb), (-xb, yb)], 1.2)
solid = fillet_vertical(solid, [(-PLATE_W / 2, fBot[1]),
                                (PLATE_W / 2, fBot[1])], 0.3)
base = cq.Workplane("XY").add(solid)

# ---------------- triangular windows ----------------
xe = -PLATE_W / 2


def offset_line(p, d, off):
    # inward normal for the left-side arms points to +X
    n = (-d[1], d[0])
    if n[0] < 0:
        n = (-n[0], -n[1])
    return (p[0] + n[0] * off, p[1] + n[1] * off), d


def line_at_y(p, d, y):
    t = (y - p[1]) / d[1]
    return (p[0] + t * d[0], y)


def line_at_x(p, d, x):
    t = (x - p[0]) / d[0]
    return (x, p[1] + t * d[1])


pb, db = offset_line(tB, dB, ARM_W)
yt = B[1] - POST_R
tri_back = [line_at_y(pb, db, yt), (xe, yt), line_at_x(pb, db, xe)]
pf, df = offset_line(tF, dF, ARM_W)
yf = F[1] + POST_R
tri_front = [line_at_y(pf, df, yf), (xe, yf), line_at_x(pf, df, xe)]


def tri_prism(pts):
    w = (cq.Workplane("XY").workplane(offset=-1)
         .polyline(pts).close().extrude(T_PLATE + 2))
    return w.edges("|Z").fillet(TRI_R)


for tri in (tri_back, tri_front):
    base = base.cut(tri_prism(tri))
    base = base.cut(tri_prism([mx(p) for p in tri]))


# ---------------- curved ribs ----------------
def wall(y_c, x_half, radius, thick, dip):
    z0 = T_PLATE - 0.5
    box = (cq.Workplane("XY")
           .box(2 * x_half, thick, TAB_BOT - z0, centered=(True, True, False))
           .translate((0, y_c, z0)))
    zc = T_PLATE - dip + radius
    cyl = cq.Solid.makeCylinder(radius, 20, cq.Vector(0, y_c - 10, zc),
                                cq.Vector(0, 1, 0))
    return box.cut(cq.Workplane("XY").add(cyl))


base = base.union(wall(FRONT_POST[1], FRONT_POST[0], WALL_R_FRONT,
                       WALL_T_FRONT, WALL_DIP_FRONT))
base = base.union(wall(BACK_POST[1], BACK_POST[0], WALL_R_BACK,
                       WALL_T_BACK, WALL_DIP_BACK))

# ---------------- posts and tabs ----------------
for sx in (1, -1):
    for post, hole in (((sx * BACK_POST[0], BACK_POST[1]), (sx * HOLE_X, HOLE_Y)),
                       ((sx * FRONT_POST[0], FRONT_POST[1]), (sx * HOLE_X, -HOLE_Y))):
        p = (cq.Workplane("XY").center(*post).circle(POST_R)
             .extrude(TAB_BOT + 0.5))
        base = base.union(p)
        ux = (post[0] - hole[0]) / POST_OFF
        uy = (post[1] - hole[1]) / POST_OFF
        mid = (hole[0] + ux * TAB_C / 2, hole[1] + uy * TAB_C / 2)
        ang = math.degrees(math.atan2(uy, ux))
        tab = (cq.Workplane("XY").workplane(offset=TAB_BOT)
               .center(*mid)
               .slot2D(TAB_C + 2 * TAB_R, 2 * TAB_R, ang)
               .extrude(TAB_T)
               .faces(">Z").edges().fillet(TAB_EDGE_R))
        base = base.union(tab)

# holes with small chamfers
for hx, hy in ((HOLE_X, HOLE_Y), (-HOLE_X, HOLE_Y), (HOLE_X, -HOLE_Y), (-HOLE_X, -HOLE_Y)):
    h = (cq.Workplane("XY").workplane(offset=TAB_BOT - 1)
         .center(hx, hy).circle(HOLE_D / 2).extrude(TAB_T + 2))
    base = base.cut(h)
    # cone: wide at top
    cs = cq.Solid.makeCone(HOLE_D / 2 - 0.01, HOLE_D / 2 + HOLE_CH + 0.5,
                           HOLE_CH + 0.5 + 0.01,
                           cq.Vector(hx, hy, TAB_TOP - HOLE_CH - 0.01),
                           cq.Vector(0, 0, 1))
    base = base.cut(cq.Workplane("XY").add(cs))
    cb = (cq.Workplane("XY").workplane(offset=TAB_BOT - 1)
          .center(hx, hy).circle(CB_D / 2).extrude(CB_DEPTH + 1))
    base = base.cut(cb)

# ---------------- blend the ribs into the posts ----------------
POSTS = [(sx * BACK_POST[0], BACK_POST[1]) for sx in (1, -1)] + \
        [(sx * FRONT_POST[0], FRONT_POST[1]) for sx in (1, -1)]


def _on_post(v, tol=0.05):
    return any(abs(math.hypot(v.x - p[0], v.y - p[1]) - POST_R) < tol for p in POSTS)


solid = base.val()
rib_post_edges = []
for e in solid.Edges():
    if e.geomType() not in ("LINE", "BSPLINE"):
        continue
    pts = [e.positionAt(t) for t in (0.0, 0.5, 1.0)]
    if all(_on_post(p) for p in pts):
        zs = [p.z for p in pts]
        if min(zs) > T_PLATE - 1e-3 and max(zs) < TAB_BOT - 0.1:
            rib_post_edges.append(e)
if rib_post_edges:
    try:
        solid = solid.fillet(RIB_POST_FILLET, rib_post_edges)
    except Exception:
        pass
base = cq.Workplane("XY").add(solid)

result = base
VIEW = {"azimuth": 45, "elevation": 26}
